import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
R_FLANGE = 25.0        # flange outer radius
R_FRONT_FLAT = 17.2    # flat front face ends here, then tapers to the rim
RIM_FRONT_Y = 2.45     # axial position of rim front edge (taper depth)
RIM_T = 0.68           # rim thickness
R_STEP_OUT = 21.75     # back-side step, outer radius
R_STEP_IN = 20.15      # back-side step, inner radius (after chamfer)
FLANGE_BACK_Y = 4.75   # back face of the thick flange region

R_BOSS = 11.93         # boss outer radius
BOSS_END_Y = 26.2      # end of boss (overall length)
BOSS_CHAMFER = 2.5     # 45 deg chamfer at boss end

R_BORE = 10.0          # blind bore from the front
END_WALL = 4.1         # thickness of the boss end wall (bore floor -> end)
ENTRY_R = 1.6          # rounded bore entry
BLEND = 0.15           # half length of the soft flat->taper transition

R_KEY = 4.9            # keyhole circle radius
SLOT_HALF_W = 4.3      # keyhole slot half width
R_SLOT_END = 14.3      # slot bottom is an arc of this radius about the axis
SLOT_CORNER_R = 1.1    # slot bottom corner radius

BORE_DEPTH = BOSS_END_Y - END_WALL
RIM_BACK_Y = RIM_FRONT_Y + RIM_T

# ---------------- revolved body (axis = +Y, front face at Y=0) ----------------
# front surface = one smooth spline: bore-entry round -> flat face -> taper to rim
taper_dir = (R_FLANGE - R_FRONT_FLAT, RIM_FRONT_Y)
tl = math.hypot(*taper_dir)
tdx, tdy = taper_dir[0] / tl, taper_dir[1] / tl
c45 = math.cos(math.radians(45))
front_pts = [
    (R_BORE, ENTRY_R),
    (R_BORE + ENTRY_R * (1 - c45), ENTRY_R * (1 - c45)),
    (R_BORE + ENTRY_R, 0.0),
    (R_FRONT_FLAT - BLEND, 0.0),
    (R_FRONT_FLAT + BLEND * tdx, BLEND * tdy),
    (R_FLANGE, RIM_FRONT_Y),
]
front_tans = [
    (0.0, -1.0),
    (c45, -c45),
    (1.0, 0.0),
    (1.0, 0.0),
    (tdx, tdy),
    (tdx, tdy),
]

# profile plane: local x = radial (pointing to -Z), local y = +Y (axis); putting the
# revolve seam at -Z means the keyhole slot removes most of it
prof_plane = cq.Plane(origin=(0, 0, 0), xDir=(0, 0, -1), normal=(1, 0, 0))
profile = (
    cq.Workplane(prof_plane)
    .moveTo(0.0, BORE_DEPTH)
    .lineTo(R_BORE, BORE_DEPTH)
    .lineTo(R_BORE, ENTRY_R)
    .spline(front_pts[1:], tangents=front_tans, includeCurrent=True)
    .lineTo(R_FLANGE, RIM_BACK_Y)
    .lineTo(R_STEP_OUT, RIM_BACK_Y)
    .lineTo(R_STEP_IN, FLANGE_BACK_Y)
    .lineTo(R_BOSS, FLANGE_BACK_Y)
    .lineTo(R_BOSS, BOSS_END_Y - BOSS_CHAMFER)
    .lineTo(R_BOSS - BOSS_CHAMFER, BOSS_END_Y)
    .lineTo(0.0, BOSS_END_Y)
    .close()
)
body = profile.revolve(360, (0, 0, 0), (0, 1, 0))

# ---------------- keyhole through everything ----------------
# XZ workplane: local x = +X, local y = +Z, normal = -Y
L = BOSS_END_Y + 10.0
key_circle = cq.Workplane("XZ").workplane(offset=5.0).circle(R_KEY).extrude(-L)

slot_rect = (
    cq.Workplane("XZ")
    .workplane(offset=5.0)
    .center(0, -R_SLOT_END / 2.0)
    .rect(2 * SLOT_HALF_W, R_SLOT_END)
    .extrude(-L)
)
slot_disc = cq.Workplane("XZ").workplane(offset=5.0).circle(R_SLOT_END).extrude(-L)
slot = slot_rect.intersect(slot_disc)
slot = slot.edges("|Y").edges(cq.selectors.BoxSelector((-SLOT_HALF_W - 0.1, -20, -R_SLOT_END - 0.1),
                                                       (SLOT_HALF_W + 0.1, 50, -R_SLOT_END + 2.0))).fillet(SLOT_CORNER_R)

body = body.cut(key_circle).cut(slot)

result = body
